import cadquery as cq

# Round snap-in cap: stepped disc (top flange + lower spigot ring) with a
# hollow underside, a locating notch, and two hooked snap legs underneath.

# ---------------- driving dimensions (mm) ----------------
R_FLANGE = 50.0        # top flange radius
T_FLANGE = 5.35        # top flange thickness
R_RING = 47.3          # lower ring (spigot) radius
T_RING = 5.2           # lower ring height
R_RECESS = 43.5        # underside recess radius (rim inner radius)
RECESS_D = 5.0         # underside recess depth (from ring bottom)

HOLE_D = 3.6           # centre through hole

POCKET_R = 10.6        # shallow round pocket in the recess floor (centre)
POCKET_D = 1.55
SLOT_L = 10.6          # two blind slots in the pocket ceiling (along X)
SLOT_W = 2.5
SLOT_X = 0.0
SLOT_Y = 4.8           # slot centre offset |Y|
SLOT_D = 1.0

NOTCH_W = 6.7          # locating notch in flange underside (+X side)
NOTCH_Y0 = 0.0         # notch starts at Y=0 and runs toward +Y
NOTCH_H = 2.4          # notch height measured up from the flange underside

LEG_W = 26.9           # snap legs (plates parallel to XZ)
LEG_T = 6.75           # full thickness
LEG_Y_OUT = 22.0       # outer face |Y|
LEG_LEN = 55.6         # below ring bottom
LEG_RELIEF_T = 2.55    # relief on inner face of lower leg
LEG_RELIEF_TOP = 35.3  # relief starts this far below ring bottom
FOOT_H = 2.6           # hook foot height at the tip

BAR_W = 4.0            # gusset bars outside each leg
BAR_X = 0.6            # bar centre X offset
BAR_Y_OUT_NEG = 38.3   # bar outer end on the -Y side
BAR_Y_OUT_POS = 36.8   # bar outer end on the +Y side
BAR_DROP = 1.45        # bar protrudes below ring bottom

SEAM_OUTER = 135.0     # revolve seam angles (placed where they show least)
SEAM_INNER = 45.0

H_TOTAL = T_RING + T_FLANGE
POCKET_TOP = RECESS_D + POCKET_D

# ---------------- revolved body ----------------
# outer disc: flange + lower ring
outer_profile = [
    (0.0, 0.0),
    (R_RING, 0.0),
    (R_RING, T_RING),
    (R_FLANGE, T_RING),
    (R_FLANGE, H_TOTAL),
    (0.0, H_TOTAL),
]
body = (cq.Workplane("XZ").polyline(outer_profile).close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), SEAM_OUTER))

# underside void: recess, central round pocket and through hole
void_profile = [
    (0.0, -1.0),
    (R_RECESS, -1.0),
    (R_RECESS, RECESS_D),
    (POCKET_R, RECESS_D),
    (POCKET_R, POCKET_TOP),
    (HOLE_D / 2, POCKET_TOP),
    (HOLE_D / 2, H_TOTAL + 1.0),
    (0.0, H_TOTAL + 1.0),
]
void = (cq.Workplane("XZ").polyline(void_profile).close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), SEAM_INNER))
body = body.cut(void)

# two blind slots in the pocket ceiling
slots = (cq.Workplane("XY").workplane(offset=POCKET_TOP - 0.01)
         .pushPoints([(SLOT_X, SLOT_Y), (SLOT_X, -SLOT_Y)])
         .rect(SLOT_L, SLOT_W).extrude(SLOT_D + 0.01))
body = body.cut(slots)

# locating notch in the flange underside at +X
# (flat back wall tangent to the ring at its start edge)
notch_len = R_FLANGE - R_RING + 2.0
notch = (cq.Workplane("XY").workplane(offset=T_RING)
         .center(R_RING + notch_len / 2, NOTCH_Y0 + NOTCH_W / 2)
         .rect(notch_len, NOTCH_W).extrude(NOTCH_H))
body = body.cut(notch)


# ---------------- snap legs ----------------
def make_leg(sign):
    """Leg plate at Y side `sign` (+1 / -1), inner face toward Y=0."""
    y_out = sign * LEG_Y_OUT
    y_in = sign * (LEG_Y_OUT - LEG_T)
    z_top = RECESS_D + 0.01
    z_bot = -LEG_LEN
    leg = (cq.Workplane("XY")
           .box(LEG_W, LEG_T, z_top - z_bot, centered=(True, True, False))
           .translate((0, (y_out + y_in) / 2, z_bot)))
    # relief on the inner face between the step and the hook foot
    rz_top = -LEG_RELIEF_TOP
    rz_bot = z_bot + FOOT_H
    relief = (cq.Workplane("XY")
              .box(LEG_W + 2, LEG_RELIEF_T, rz_top - rz_bot,
                   centered=(True, True, False))
              .translate((0, y_in + sign * LEG_RELIEF_T / 2, rz_bot)))
    leg = leg.cut(relief)
    # gusset bar on the outer face, tied into the recess floor
    bar_len = (BAR_Y_OUT_POS if sign > 0 else BAR_Y_OUT_NEG) - LEG_Y_OUT
    bar = (cq.Workplane("XY")
           .box(BAR_W, bar_len + 0.01, RECESS_D + BAR_DROP + 0.01,
                centered=(True, True, False))
           .translate((BAR_X, sign * (LEG_Y_OUT + bar_len / 2), -BAR_DROP)))
    return leg.union(bar)


result = body.union(make_leg(1)).union(make_leg(-1))

VIEW = {"azimuth": 45, "elevation": 26}
